import math
import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
# hexagonal body
HEX_HALF_W = 87.7      # half width at the side vertices (X)
HEX_VERT_Y = 29.2      # half length of the side (vertical) edges
HEX_FLAT_XF = 29.0     # half width of the front flat edge (hidden in the pillar)
HEX_FLAT_XB = 30.8     # half width of the back flat edge (hidden in the housing)
HEX_FLAT_Y = 72.3      # Y of the front/back flat edges
HEX_Z0, HEX_Z1 = 26.6, 76.5

# spine / servo housing (stadium in plan)
SPINE_W = 31.5         # half width
HOUSING_CY = 76.5      # centre of the rounded back
HOUSING_Z0 = 13.2
HOUSING_FILLET = 4.0

# pillar of the C bracket
PIL_Y0, PIL_Y1 = -74.8, -39.8
PIL_TOP = 110.5
PIL_CONCAVE = 6.0
PIL_EDGE_R = 3.0
PIL_BASE_R = 6.0

# top plate
AXIS_Y = -103.6        # servo horn axis
TP_Z0, TP_Z1 = 110.5, 116.9
TP_REAR_Y = -53.3
TP_SIDE_Y = -75.0
TP_R = 25.8
TP_HOLE_D = 12.6
TP_SMALL_PCD_R = 20.6
TP_SMALL_D = 4.2
TP_FILLET = 2.0
TP_REAR_R = 5.0

# under-plate reinforcement
UB_Z0 = 104.1
UB_CUT_R = 28.5

# bottom plate
BP_Z0, BP_Z1 = 0.0, 11.2
BP_R_FRONT = 19.6
BP_SIDE_Y = -80.0
BP_REAR_END = 11.5
BP_HOLE_D = 13.0
BP_FILLET = 5.0

# pin under the housing
PIN_Y = 74.0
PIN_D = 12.0
PIN_HOLE_D = 6.0

# housing pocket
POCKET_FLOOR = 18.6
WIN_TOP = 71.0
WIN_BOT = 19.2
WIN_R = 1.8
POCKET_Y0 = 10.3
TRUSS_DEPTH = 3.0
TRUSS_DX = 2.0
GAP_R = 2.5
GAP_Y = 0.3
GAP_DEPTH = 8.0
BACK_CAV_TOP = 69.0
BACK_CAV_X0 = -6.0
WALL_IN = 27.7         # inner face of the side walls in the wide bays
POCKET_NARROW = 20.8   # half width of the front (narrow) section
POCKET_RIB = 21.0      # inner face of the mid rib / rear narrow section
POCKET_Y_STEPS = (24.9, 49.9, 56.0, 80.7, 96.0)


def tangent_point(px, py, cx, cy, r, sign):
    dx, dy = px - cx, py - cy
    d = math.hypot(dx, dy)
    th = math.atan2(dy, dx)
    a = math.acos(r / d)
    ang = th + sign * a
    return (cx + r * math.cos(ang), cy + r * math.sin(ang))


def d_shape(w, y_rear, y_side, cy, r, z0, h):
    """Plate outline: straight rear edge, straight sides, tapering to a front arc."""
    tr = tangent_point(w, y_side, 0.0, cy, r, -1)
    tl = (-tr[0], tr[1])
    return (
        cq.Workplane("XY").workplane(offset=z0)
        .moveTo(w, y_rear)
        .lineTo(w, y_side)
        .lineTo(*tr)
        .threePointArc((0.0, cy - r), tl)
        .lineTo(-w, y_side)
        .lineTo(-w, y_rear)
        .close()
        .extrude(h)
    )


def zcyl(x, y, d, z0, h):
    return cq.Workplane("XY").workplane(offset=z0).center(x, y).circle(d / 2).extrude(h)


def prism_yz(poly, x0, x1, r=0.0):
    """Prism from a (corner-rounded) polygon in the (Y, Z) plane, spanning x0..x1."""
    sk = cq.Sketch().polygon(list(poly) + [poly[0]])
    if r > 0:
        sk = sk.vertices().fillet(r)
    return cq.Workplane("YZ").workplane(offset=x0).placeSketch(sk).extrude(x1 - x0)


# ---------------- hex body ----------------
hex_pts = [
    (HEX_HALF_W, -HEX_VERT_Y), (HEX_HALF_W, HEX_VERT_Y),
    (HEX_FLAT_XB, HEX_FLAT_Y), (-HEX_FLAT_XB, HEX_FLAT_Y),
    (-HEX_HALF_W, HEX_VERT_Y), (-HEX_HALF_W, -HEX_VERT_Y),
    (-HEX_FLAT_XF, -HEX_FLAT_Y), (HEX_FLAT_XF, -HEX_FLAT_Y),
]
hex_body = (
    cq.Workplane("XY").workplane(offset=HEX_Z0)
    .polyline(hex_pts).close().extrude(HEX_Z1 - HEX_Z0)
)
# keep the hex nose tucked behind the concave face of the pillar
_rc = (SPINE_W ** 2 + PIL_CONCAVE ** 2) / (2 * PIL_CONCAVE)
hex_body = hex_body.cut(
    cq.Workplane("XY").workplane(offset=HEX_Z0 - 1)
    .center(0, PIL_Y0 + PIL_CONCAVE - _rc).circle(_rc + 1.0).extrude(HEX_Z1 - HEX_Z0 + 2)
)

# ---------------- spine + housing (stadium) ----------------
spine = (
    cq.Workplane("XY").workplane(offset=HOUSING_Z0)
    .moveTo(SPINE_W, PIL_Y1)
    .lineTo(SPINE_W, HOUSING_CY)
    .threePointArc((0, HOUSING_CY + SPINE_W), (-SPINE_W, HOUSING_CY))
    .lineTo(-SPINE_W, PIL_Y1)
    .close()
    .extrude(HEX_Z1 - HOUSING_Z0)
)

# ---------------- bottom plate ----------------
rear_cy = BP_REAR_END - SPINE_W
tr = tangent_point(SPINE_W, BP_SIDE_Y, 0.0, AXIS_Y, BP_R_FRONT, -1)
bottom_plate = (
    cq.Workplane("XY").workplane(offset=BP_Z0)
    .moveTo(SPINE_W, rear_cy)
    .lineTo(SPINE_W, BP_SIDE_Y)
    .lineTo(*tr)
    .threePointArc((0.0, AXIS_Y - BP_R_FRONT), (-tr[0], tr[1]))
    .lineTo(-SPINE_W, BP_SIDE_Y)
    .lineTo(-SPINE_W, rear_cy)
    .threePointArc((0.0, BP_REAR_END), (SPINE_W, rear_cy))
    .close()
    .extrude(HOUSING_Z0 - BP_Z0)
)
bottom_plate = bottom_plate.faces("<Z").edges().fillet(BP_FILLET)
# the part of the plate in front of the pillar is only BP_Z1 thick
bottom_plate = bottom_plate.cut(
    cq.Workplane("XY").workplane(offset=BP_Z1)
    .center(0, (-150 + PIL_Y0 + PIL_EDGE_R + 4.0) / 2)
    .rect(100, PIL_Y0 + PIL_EDGE_R + 4.0 + 150).extrude(20)
)


def edges_at_z(wp, z, pred):
    sel = []
    for e in wp.edges().vals():
        bb = e.BoundingBox()
        if abs(bb.zmin - z) < 0.01 and abs(bb.zmax - z) < 0.01 and pred(e, bb):
            sel.append(e)
    return wp.newObject(sel)


# spine sits on the rear of the plate: blend the joint, then round the housing bottom
base = spine.union(bottom_plate)
base = edges_at_z(
    base, HOUSING_Z0,
    lambda e, bb: e.geomType() == "CIRCLE" and bb.ymin > rear_cy - 1 and bb.ymax < BP_REAR_END + 1,
).fillet(3.0)
base = edges_at_z(
    base, HOUSING_Z0,
    lambda e, bb: bb.ymin > rear_cy - 5 and (e.geomType() == "LINE" or bb.ymin > HOUSING_CY - 1),
).fillet(HOUSING_FILLET)

# ---------------- pillar ----------------
pillar = (
    cq.Workplane("XY").workplane(offset=BP_Z1)
    .center(0, (PIL_Y0 + PIL_Y1) / 2)
    .rect(2 * SPINE_W, PIL_Y1 - PIL_Y0)
    .extrude(PIL_TOP - BP_Z1)
)
# concave front face
rc = (SPINE_W ** 2 + PIL_CONCAVE ** 2) / (2 * PIL_CONCAVE)
concave = (
    cq.Workplane("XY").workplane(offset=BP_Z1 - 5)
    .center(0, PIL_Y0 + PIL_CONCAVE - rc)
    .circle(rc).extrude(PIL_TOP - BP_Z1 + 5)
)
pillar = pillar.cut(concave)

# pillar + bottom plate with a generous root fillet, then round the front corners
bracket = pillar.union(base)
bracket = bracket.edges(
    cq.selectors.BoxSelector((-31.0, PIL_Y0 - 1.0, BP_Z1 - 0.5), (31.0, PIL_Y0 + PIL_CONCAVE + 1.0, BP_Z1 + 0.5))
).fillet(PIL_BASE_R)
bracket = bracket.edges("|Z").edges(
    cq.selectors.BoxSelector((-40, PIL_Y0 - 1.0, 20.0), (40, PIL_Y0 + 0.5, 100.0))
).fillet(PIL_EDGE_R)

# ---------------- top plate ----------------
top_plate = d_shape(SPINE_W, TP_REAR_Y, TP_SIDE_Y, AXIS_Y, TP_R, TP_Z0, TP_Z1 - TP_Z0)
# generous round-over along the rear edge where the plate sits on the pillar head
rr = TP_REAR_R
top_plate = top_plate.cut(
    cq.Workplane("YZ").workplane(offset=-40)
    .center(TP_REAR_Y - rr / 2 + 0.5, TP_Z1 - rr / 2 + 0.5).rect(rr + 1, rr + 1).extrude(80)
    .cut(cq.Workplane("YZ").workplane(offset=-41).center(TP_REAR_Y - rr, TP_Z1 - rr).circle(rr).extrude(82))
)
# small round on the remaining top edges (incl. the ends of the rear round-over)
_sel = []
for e in top_plate.edges().vals():
    bb, c = e.BoundingBox(), e.Center()
    top_edge = abs(bb.zmax - TP_Z1) < 0.01 and abs(bb.zmin - TP_Z1) < 0.01 and c.y < TP_REAR_Y - rr - 0.5
    side_arc = (abs(abs(c.x) - SPINE_W) < 0.01 and bb.ymin >= TP_REAR_Y - rr - 0.01
                and bb.zmin > TP_Z0 + 0.01 and e.geomType() == "CIRCLE")
    if top_edge or side_arc:
        _sel.append(e)
top_plate = top_plate.newObject(_sel).fillet(TP_FILLET)

under_block = d_shape(SPINE_W, PIL_Y0 + PIL_CONCAVE + 1.5, TP_SIDE_Y, AXIS_Y, TP_R, UB_Z0, TP_Z0 - UB_Z0 + 0.5)
under_block = under_block.cut(zcyl(0, AXIS_Y, 2 * UB_CUT_R, UB_Z0 - 1, 20))
# let the rounded front corners of the pillar run up to the plate
for sgn in (1, -1):
    cx = sgn * (SPINE_W - PIL_EDGE_R)
    corner = (
        cq.Workplane("XY").workplane(offset=UB_Z0 - 1)
        .center(cx + sgn * PIL_EDGE_R / 2 + sgn * 0.5, PIL_Y0 + PIL_EDGE_R / 2)
        .rect(PIL_EDGE_R + 1.0, PIL_EDGE_R).extrude(TP_Z0 - UB_Z0 + 1)
        .cut(zcyl(cx, PIL_Y0 + PIL_EDGE_R, 2 * PIL_EDGE_R, UB_Z0 - 2, 20))
    )
    under_block = under_block.cut(corner)

# ---------------- pin ----------------
pin = zcyl(0, PIN_Y, PIN_D, 0.0, HOUSING_Z0 + 2.0)

# ---------------- housing: hex body + spine, pocket and truss windows ----------------
housing = hex_body.union(bracket)

_y1, _y2, _y3, _y4, _y5 = POCKET_Y_STEPS
pocket_pts = [
    (POCKET_NARROW, POCKET_Y0), (POCKET_NARROW, _y1), (WALL_IN, _y1), (WALL_IN, _y2), (POCKET_RIB, _y2),
    (POCKET_RIB, _y3), (WALL_IN, _y3), (WALL_IN, _y4), (POCKET_RIB, _y4), (POCKET_RIB, _y5),
]
pocket_pts = pocket_pts + [(-x, y) for (x, y) in reversed(pocket_pts)]
pocket = (
    cq.Workplane("XY").workplane(offset=POCKET_FLOOR)
    .polyline(pocket_pts).close().extrude(HEX_Z1 - POCKET_FLOOR + 1)
)
housing = housing.cut(pocket)

# truss windows through the housing side walls (polygons in the Y-Z plane)
windows = [
    # middle bay
    [(31.0, WIN_TOP), (48.0, WIN_TOP), (48.0, 44.0), (31.0, 63.0)],
    [(23.5, WIN_BOT), (48.0, WIN_BOT), (23.5, 59.0)],
    # rear bay
    [(56.0, WIN_TOP), (80.0, WIN_TOP), (80.0, 35.0)],
    [(54.7, WIN_BOT), (79.6, WIN_BOT), (54.7, 55.5)],
]
for w in windows:
    for sgn in (1, -1):
        x0, x1 = (WALL_IN - 0.5, SPINE_W + 1.0) if sgn > 0 else (-SPINE_W - 1.0, -WALL_IN + 0.5)
        housing = housing.cut(prism_yz(w, x0, x1, WIN_R))

# shallow Warren-truss recesses on the front wall of the pocket
truss = [
    [(-7.5, 67.0), (7.5, 67.0), (0.0, 54.0)],
    [(3.5, 50.0), (16.0, 50.0), (10.5, 62.0)],
    [(-3.5, 54.0), (-18.0, 54.0), (-11.0, 67.0)],
]
for t in truss:
    t = [(x + TRUSS_DX, z) for (x, z) in t]
    sk = cq.Sketch().polygon(list(t) + [t[0]]).vertices().fillet(1.0)
    housing = housing.cut(
        cq.Workplane("XZ").workplane(offset=-(POCKET_Y0 + 0.5)).placeSketch(sk).extrude(TRUSS_DEPTH + 0.5)
    )

# tiny corner gaps where the housing meets the hex deck
for sgn in (1, -1):
    cx = sgn * (SPINE_W - GAP_R)
    gap = (
        cq.Workplane("XY").workplane(offset=HEX_Z1 - GAP_DEPTH)
        .center(cx + sgn * GAP_R / 2, GAP_Y + GAP_R / 2)
        .rect(GAP_R, GAP_R).extrude(GAP_DEPTH + 1)
        .cut(zcyl(cx, GAP_Y + GAP_R, 2 * GAP_R, HEX_Z1 - GAP_DEPTH - 1, GAP_DEPTH + 3))
    )
    housing = housing.cut(gap)

# housing top holes
hh = [(-11.0, 99.9, 5.5), (11.0, 99.9, 5.5), (-26.2, 85.7, 5.0), (26.2, 85.7, 5.0),
      (-26.2, 17.7, 5.0), (26.2, 17.7, 5.0), (-11.3, 6.1, 6.5), (11.3, 6.1, 6.5)]
for (x, y, d) in hh:
    housing = housing.cut(zcyl(x, y, d, HEX_Z1 - 12, 14))
    # 118 deg drill point at the bottom of each blind hole
    tip = d / 2 / math.tan(math.radians(59))
    housing = housing.cut(
        cq.Solid.makeCone(d / 2, 0.0, tip, cq.Vector(x, y, HEX_Z1 - 12), cq.Vector(0, 0, -1))
    )

# undercut cavity behind the rear pocket wall, following the rounded back
back_cav = (
    cq.Workplane("XY").workplane(offset=POCKET_FLOOR)
    .center(0, HOUSING_CY).circle(SPINE_W - 3.5).extrude(BACK_CAV_TOP - POCKET_FLOOR)
    .intersect(
        cq.Workplane("XY").workplane(offset=POCKET_FLOOR)
        .center((BACK_CAV_X0 + POCKET_RIB) / 2, _y5 - 1.0 + 10.0)
        .rect(POCKET_RIB - BACK_CAV_X0, 20.0).extrude(BACK_CAV_TOP - POCKET_FLOOR)
    )
)
housing = housing.cut(back_cav)

# boss with bore at the pocket floor (pin axis)
housing = housing.union(zcyl(0, PIN_Y, 9.0, POCKET_FLOOR - 0.5, 3.5))

# ---------------- assemble ----------------
body = housing.union(top_plate).union(under_block).union(pin)

# ---------------- holes ----------------
cutters = []
# top plate
cutters.append(zcyl(0, AXIS_Y, TP_HOLE_D, UB_Z0 - 5, 30))
for ang in (0, 90, 180, 270):
    x = TP_SMALL_PCD_R * math.cos(math.radians(ang))
    y = AXIS_Y + TP_SMALL_PCD_R * math.sin(math.radians(ang))
    cutters.append(zcyl(x, y, TP_SMALL_D, UB_Z0 - 5, 30))
# counterbored screw holes (plate corners and pillar head)
for (x, y, ztop) in ((-26.0, -66.5, TP_Z1), (26.0, -66.5, TP_Z1), (0.0, -46.8, PIL_TOP)):
    cutters.append(zcyl(x, y, 3.8, ztop - 20, 25))
    cutters.append(zcyl(x, y, 7.0, ztop - 3.0, 6))
# side hole through the pillar head
cutters.append(
    cq.Workplane("YZ").workplane(offset=-40).center(-56.8, 99.9).circle(2.6).extrude(80)
)
# bottom plate hole
cutters.append(zcyl(0, AXIS_Y, BP_HOLE_D, -1, BP_Z1 + 2))
# pin bore
cutters.append(zcyl(0, PIN_Y, PIN_HOLE_D, -1, 10))
cutters.append(zcyl(0, PIN_Y, 4.0, POCKET_FLOOR - 8, 14))
for c in cutters:
    body = body.cut(c)

result = body
